import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
FLANGE_D = 80.0        # flange disc diameter
FLANGE_T = 3.9         # flange thickness
TUBE_OD = 46.9         # collar outer diameter
TUBE_ID = 39.2         # collar inner diameter (through bore)
TUBE_H = 17.5          # collar height above flange
BASE_FILLET = 2.2      # collar-to-flange fillet radius
RIM_R = 1.6            # rounding of collar top rim (both edges)

SPOKE_T = 4.4          # thickness of the three internal ribs at the bottom
SPOKE_T_TOP = 3.0      # rib thickness at the top (drafted rib sides)
SPOKE_CORNER_R = 1.0   # vertical fillet where the ribs meet at the centre
SPOKE_TOP_R = 1.0      # rounding of the rib top edges
SPOKE_ANGLE0 = -64.5   # angle of first rib / lug (deg from +X)

LUG_W = 12.4           # lug tangential width (two wide lugs)
LUG_W_NARROW = 11.1    # width of the third, narrower (keying) lug
LUG_H = 8.5            # lug height (from collar top downwards)
LUG_OUT = 26.8         # radius of lug outer face
LUG_RV = 2.4           # lug vertical-edge rounding
LUG_RH = 1.8           # lug top/bottom edge rounding
LUG_JOIN_R = 1.0       # lug-to-collar fillet

TOTAL_H = FLANGE_T + TUBE_H
RO = TUBE_OD / 2.0
RI = TUBE_ID / 2.0
ANGLES = [SPOKE_ANGLE0 + 120.0 * i for i in range(3)]
# lugs sit on the rib ends, with small individual angular offsets (keyed)
LUG_OFFSETS = [2.0, -1.5, 0.5]
LUG_ANGLES = [a + d for a, d in zip(ANGLES, LUG_OFFSETS)]
LUG_WIDTHS = [LUG_W, LUG_W, LUG_W_NARROW]


def pol(r, a_deg):
    a = math.radians(a_deg)
    return (r * math.cos(a), r * math.sin(a))


def off(p, q):
    return (p[0] + q[0], p[1] + q[1])


def scl(v, s):
    return (v[0] * s, v[1] * s)


# ---------------- revolved body: flange + collar ----------------
# half profile in the XZ plane (x = radius), revolved about Z
prof = (
    cq.Workplane("XZ")
    .moveTo(RI, 0)
    .lineTo(FLANGE_D / 2.0, 0)
    .lineTo(FLANGE_D / 2.0, FLANGE_T)
    .lineTo(RO + BASE_FILLET, FLANGE_T)
    .radiusArc((RO, FLANGE_T + BASE_FILLET), BASE_FILLET)
    .lineTo(RO, TOTAL_H - RIM_R)
    .radiusArc((RO - RIM_R, TOTAL_H), -RIM_R)
    .lineTo(RI + RIM_R, TOTAL_H)
    .radiusArc((RI, TOTAL_H - RIM_R), -RIM_R)
    .close()
)
body = prof.revolve(360, (0, 0, 0), (0, 1, 0))

# ---------------- internal ribs (three-spoke star) ----------------
h = SPOKE_T / 2.0
L = RI + 2.0                      # ribs run into the collar wall
r = SPOKE_CORNER_R
D = (h + r) / math.sin(math.radians(60))
t = (h + r) / math.tan(math.radians(60))

pts_seq = []
for i, a in enumerate(ANGLES):
    u = pol(1, a)
    n = pol(1, a + 90)
    an = ANGLES[(i + 1) % 3]
    u2 = pol(1, an)
    n2 = pol(1, an + 90)
    Pa = off(scl(u, L), scl(n, -h))
    Pb = off(scl(u, L), scl(n, h))
    T1 = off(scl(u, t), scl(n, h))
    M = pol(D - r, a + 60)
    T2 = off(scl(u2, t), scl(n2, -h))
    pts_seq.append((Pa, Pb, T1, M, T2))

sk = cq.Workplane("XY").moveTo(*pts_seq[0][0])
for i, (Pa, Pb, T1, M, T2) in enumerate(pts_seq):
    if i > 0:
        sk = sk.lineTo(*Pa)
    sk = sk.lineTo(*Pb).lineTo(*T1).threePointArc(M, T2)
sk = sk.close()
SPOKE_DRAFT = math.degrees(math.atan((SPOKE_T - SPOKE_T_TOP) / 2.0 / TOTAL_H))
star = sk.extrude(TOTAL_H, taper=SPOKE_DRAFT)
# rounded top edges on the ribs
try:
    star = star.faces(">Z").edges().fillet(SPOKE_TOP_R)
except Exception:
    try:
        star = star.faces(">Z").edges().fillet(SPOKE_TOP_R * 0.5)
    except Exception:
        pass

result = body.union(star)

# ---------------- lugs ----------------
lug_in = RI + RIM_R + 0.2
lug_depth = LUG_OUT - lug_in
def make_lug(width):
    box = (
        cq.Workplane("XY")
        .box(lug_depth, width, LUG_H)
        .edges("|Z and >X").fillet(LUG_RV)
    )
    xmin = -lug_depth / 2.0
    hz = [e for e in box.edges().vals()
          if e.BoundingBox().xmin > xmin + 1e-3 and e.BoundingBox().zlen < 1e-3]
    solid = box.val().fillet(LUG_RH, hz)
    return cq.Workplane("XY").add(solid).translate(
        ((LUG_OUT + lug_in) / 2.0, 0, TOTAL_H - LUG_H / 2.0))


for a, w in zip(LUG_ANGLES, LUG_WIDTHS):
    lug = make_lug(w).rotate((0, 0, 0), (0, 0, 1), a)
    result = result.union(lug)


# fillet the concave junction between each lug and the collar
def _lug_join_edge(e):
    bb = e.BoundingBox()
    if bb.zmax > TOTAL_H - 0.3 or bb.zmin < TOTAL_H - LUG_H - 0.5:
        return False
    c = e.Center()
    rc = math.hypot(c.x, c.y)
    if not (RO - 1.2 < rc < RO + 0.3):
        return False
    ac = math.degrees(math.atan2(c.y, c.x))
    for a in LUG_ANGLES:
        d = (ac - a + 180.0) % 360.0 - 180.0
        if abs(d) < 20.0:
            return True
    return False


try:
    join_edges = [e for e in result.edges().vals() if _lug_join_edge(e)]
    if join_edges:
        result = cq.Workplane("XY").add(result.val().fillet(LUG_JOIN_R, join_edges))
except Exception as ex:
    print("lug join fillet failed:", ex)

VIEW = {"azimuth": 45, "elevation": 26}
